import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
L = 214.0          # overall length, tip to tip
W = 30.0           # arm width (= head diameter)
T = 15.5           # arm thickness
STEP = 3.1         # head top is lowered by this much
R_BOT = 2.0        # fillet on the bottom outline

# internal spline in the head
N_TEETH = 20
D_MINOR = 16.7     # tooth tip (bore) diameter
D_MAJOR = 19.0     # groove root diameter
GROOVE_W = 1.25    # width of each round-bottom spline groove (teeth on the X axis)
R_TIP = 0.35       # rounding of the spline tooth tips

# thin label pad on the underside
PAD_X0 = 0.636     # start, fraction of L from head end
PAD_X1 = 0.911     # end, fraction of L from head end
PAD_W = 0.62 * W
PAD_T = 0.15
# engraved line on the pad
LINE_A0, LINE_A1 = 0.21, 0.97   # along the pad, fraction of pad length
LINE_B = 0.34                   # across the pad, fraction of pad width from -Y edge
LINE_W = 0.15
LINE_D = 0.08

VIEW = {"azimuth": 45, "elevation": 26}

x_head = -L / 2 + W / 2   # head centre

# ---------------- main arm ----------------
body = (
    cq.Workplane("XY")
    .slot2D(L, W)
    .extrude(T)
)
body = body.edges("<Z").fillet(R_BOT)

# lowered head top (circular step)
step_cut = (
    cq.Workplane("XY", origin=(x_head, 0, T - STEP))
    .circle(W / 2)
    .extrude(STEP + 1)
)
body = body.cut(step_cut)

# internal spline through the head: bore + round-bottom radial grooves
bore = (
    cq.Workplane("XY", origin=(x_head, 0, -5))
    .circle(D_MINOR / 2)
    .extrude(T + 10)
)
r_in = D_MINOR / 2 - 1.2
r_out = D_MAJOR / 2
g_len = r_out - r_in
grooves = (
    cq.Workplane("XY", origin=(x_head, 0, -5))
    .polarArray((r_in + r_out) / 2, 180.0 / N_TEETH, 360, N_TEETH)
    .slot2D(g_len, GROOVE_W)
    .extrude(T + 10)
)
body = body.cut(bore.union(grooves))

# round the tooth tips (vertical edges where grooves meet the bore)
def _tip_edge(e):
    c = e.Center()
    r = math.hypot(c.x - x_head, c.y)
    return abs(r - D_MINOR / 2) < 0.3

tip_edges = [e for e in body.edges("|Z").vals() if _tip_edge(e)]
body = body.newObject(tip_edges).fillet(R_TIP)

# underside label pad
px0 = -L / 2 + PAD_X0 * L
px1 = -L / 2 + PAD_X1 * L
pad = (
    cq.Workplane("XY", origin=((px0 + px1) / 2, 0, 0))
    .rect(px1 - px0, PAD_W)
    .extrude(-PAD_T)
)
body = body.union(pad)

# thin engraved line on the pad
lx0 = px0 + LINE_A0 * (px1 - px0)
lx1 = px0 + LINE_A1 * (px1 - px0)
ly = -PAD_W / 2 + LINE_B * PAD_W
line = (
    cq.Workplane("XY", origin=((lx0 + lx1) / 2, ly, -PAD_T - 1))
    .rect(lx1 - lx0, LINE_W)
    .extrude(1 + LINE_D)
)
body = body.cut(line)

result = body
